import math
import cadquery as cq

VIEW = {"azimuth": 45, "elevation": 26}

# =====================================================================
#  Round base plate with a 45 degree sensor bracket
#  (disc with three spoke cut-outs, centre hole, two small bosses and a
#   thick gusseted bracket carrying a rectangular window at 45 deg)
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
R_DISC = 100.0        # base disc radius
T_DISC = 6.5          # base disc thickness
DISC_TOP_R = 2.0      # rounding of the disc rim (top)
DISC_BOT_R = 1.0      # rounding of the disc rim (bottom)

R_IN = 42.0           # inner radius of the spoke cut-outs
R_OUT = 72.5          # outer radius of the spoke cut-outs
SPOKE_HALF = 16.0     # half width of the spokes between cut-outs
CUT_CORNER_R = 6.0    # corner radius of the cut-outs
CUT_EDGE_R = 0.0      # edge break on the cut-outs (0 = sharp)

D_CENTER = 21.0       # centre hole

BOSS_X = 34.5         # boss positions (+/- X on the Y=0 line)
BOSS_D = 10.0
BOSS_H = 10.8
BOSS_FILLET = 2.5
BOSS_HOLE_D = 2.5     # through hole
BOSS_CB_D = 3.6       # counterbore at the top of the boss
BOSS_CB_DEPTH = 4.0

# bracket (thick plate standing in the XZ plane, behind the disc centre)
BR_Y0 = 13.6          # front face
BR_Y1 = 38.6          # back face
BR_XL = -41.0         # left edge
BR_XR = 80.0          # right edge
BR_ZL = 39.0          # height of left edge (start of 45 deg slope)
BR_ZR = 91.0          # height of right edge (start of 45 deg chamfer)
SLOPE = 45.0          # slope angle of the sensor face

WIN_C = (19.6, 61.3)  # window centre (x, z above disc top)
WIN_L = 82.0          # window length along the slope
WIN_W = 41.0          # window width
POCKET_L = 116.0      # rear pocket length
POCKET_W = 45.0       # rear pocket width
POCKET_D = 6.5        # rear pocket depth
POCKET_R = 1.0
HOLE_U = 52.0         # mounting holes along slope (from window centre)
HOLE_V = 10.5         # mounting holes across slope
HOLE_D = 6.0

RIB_T = 8.5           # diagonal rib between window and triangle
TRI_XR = 68.0         # right side of triangular opening
TRI_ZB = 7.0          # bottom of triangular opening (above disc)
TRI_R = 2.5           # rounding of the two lower corners (apex stays sharp)

R_PEAK = 5.0          # rounding of the bracket apex
R_SHOULDER_L = 4.5    # rounding where the slope meets the low end
R_SHOULDER_R = 3.0    # rounding where the chamfer meets the tall end
R_FRONT_TOP = 1.2     # edge break along the sloped front outline
R_FRONT_SIDE = 7.0    # rounding of the vertical front edges
R_BASE_FRONT = 3.0    # fillet bracket -> disc, front side
R_BASE_SIDE = 5.5     # fillet bracket -> disc, left and right sides


# ---------------- helpers ----------------
class FnSel(cq.Selector):
    """Select objects for which a predicate holds."""

    def __init__(self, fn):
        self.fn = fn

    def filter(self, objectList):
        return [o for o in objectList if self.fn(o)]


def _bb(e):
    return e.BoundingBox()


def variable_fillet(shape, edges, radius_at):
    """Fillet a tangent chain of edges with a radius that may differ from
    vertex to vertex (linear blend along each edge).  radius_at(x, y, z)
    returns the radius wanted at a vertex."""
    from OCP.BRepFilletAPI import BRepFilletAPI_MakeFillet
    from OCP.TopExp import TopExp
    from OCP.BRep import BRep_Tool

    mk = BRepFilletAPI_MakeFillet(shape.wrapped)
    for e in edges:
        mk.Add(e.wrapped)
    for ic in range(1, mk.NbContours() + 1):
        for j in range(1, mk.NbEdges(ic) + 1):
            ed = mk.Edge(ic, j)
            p1 = BRep_Tool.Pnt_s(TopExp.FirstVertex_s(ed, True))
            p2 = BRep_Tool.Pnt_s(TopExp.LastVertex_s(ed, True))
            r1 = radius_at(p1.X(), p1.Y(), p1.Z())
            r2 = radius_at(p2.X(), p2.Y(), p2.Z())
            if abs(r1 - r2) < 1e-9:
                mk.SetRadius(r1, ic, j)
            else:
                mk.SetRadius(r1, r2, ic, j)
    mk.Build()
    if not mk.IsDone():
        raise RuntimeError("variable fillet failed")
    out = cq.Shape.cast(mk.Shape())
    if not out.isValid():
        raise RuntimeError("variable fillet produced an invalid solid")
    return out


# =====================================================================
#  Base disc
# =====================================================================
disc = cq.Workplane("XY").circle(R_DISC).extrude(T_DISC)
disc = disc.faces(">Z").edges().fillet(DISC_TOP_R)
disc = disc.faces("<Z").edges().fillet(DISC_BOT_R)


def sector_cutter(box_center, box_size):
    """Annular sector (R_IN..R_OUT) clipped by a box, corners rounded."""
    ring = (cq.Workplane("XY").workplane(offset=-1)
            .circle(R_OUT).circle(R_IN).extrude(T_DISC + 2))
    box = cq.Workplane("XY").box(*box_size).translate(box_center)
    c = ring.intersect(box)
    return c.edges("|Z").fillet(CUT_CORNER_R)


BIG = 2.0 * R_DISC
HZ = T_DISC + 2
cut_left = sector_cutter((-SPOKE_HALF - BIG / 2, -SPOKE_HALF - BIG / 2, T_DISC / 2), (BIG, BIG, HZ))
cut_right = sector_cutter((SPOKE_HALF + BIG / 2, -SPOKE_HALF - BIG / 2, T_DISC / 2), (BIG, BIG, HZ))
cut_back = sector_cutter((0, BIG / 2, T_DISC / 2), (2 * SPOKE_HALF, BIG, HZ))
disc = disc.cut(cut_left).cut(cut_right).cut(cut_back)


def _cut_edge(e):
    b = _bb(e)
    if b.zlen > 0.01:
        return False
    if not (abs(b.zmin - T_DISC) < 0.01 or abs(b.zmin) < 0.01):
        return False
    c = e.Center()
    return R_IN - 12 < math.hypot(c.x, c.y) < R_OUT + 2


if CUT_EDGE_R > 0:
    try:
        disc = disc.edges(FnSel(_cut_edge)).fillet(CUT_EDGE_R)
    except Exception:
        pass

disc = disc.cut(cq.Workplane("XY").circle(D_CENTER / 2).extrude(T_DISC * 3, both=True))

# ---------------- bosses ----------------
for sx in (-1, 1):
    boss = (cq.Workplane("XY").workplane(offset=T_DISC - 0.5)
            .center(sx * BOSS_X, 0).circle(BOSS_D / 2).extrude(BOSS_H + 0.5))
    disc = disc.union(boss)
try:
    disc = disc.edges(FnSel(lambda e: abs(_bb(e).zmax - T_DISC) < 0.01 and _bb(e).zlen < 0.01
                            and abs(abs(e.Center().x) - BOSS_X) < 0.5
                            and abs(e.Center().y) < 0.5)).fillet(BOSS_FILLET)
except Exception:
    pass
for sx in (-1, 1):
    hole = (cq.Workplane("XY").workplane(offset=-1)
            .center(sx * BOSS_X, 0).circle(BOSS_HOLE_D / 2).extrude(T_DISC + BOSS_H + 2))
    cbore = (cq.Workplane("XY").workplane(offset=T_DISC + BOSS_H - BOSS_CB_DEPTH)
             .center(sx * BOSS_X, 0).circle(BOSS_CB_D / 2).extrude(BOSS_CB_DEPTH + 1))
    disc = disc.cut(hole).cut(cbore)

# =====================================================================
#  Bracket
# =====================================================================
zt = T_DISC
zb = zt - 0.5                          # sink slightly into the disc
tan_s = math.tan(math.radians(SLOPE))
c1 = BR_ZL - BR_XL * tan_s             # slope line    z = x*tan + c1
c2 = BR_ZR + BR_XR                     # chamfer line  z = -x + c2
xp = (c2 - c1) / (tan_s + 1.0)         # apex
zp = xp * tan_s + c1
prof = [
    (BR_XL, 0.0),
    (BR_XR, 0.0),
    (BR_XR, BR_ZR),
    (xp, zp),
    (BR_XL, BR_ZL),
]
depth = BR_Y1 - BR_Y0
ym = (BR_Y0 + BR_Y1) / 2.0
NP = cq.selectors.NearestToPointSelector

# side profile extruded front-to-back, apex and shoulders rounded
side = (cq.Workplane("XZ", origin=(0, BR_Y1, zb))
        .polyline(prof).close()
        .extrude(depth))
side = side.edges("|Y").edges(NP((xp, ym, zb + zp))).fillet(R_PEAK)
side = side.edges("|Y").edges(NP((BR_XR, ym, zb + BR_ZR))).fillet(R_SHOULDER_R)
side = side.edges("|Y").edges(NP((BR_XL, ym, zb + BR_ZL))).fillet(R_SHOULDER_L)

# plan footprint extruded upwards, the two front vertical corners rounded
plan = (cq.Workplane("XY", origin=(0, 0, zb - 1))
        .center((BR_XL + BR_XR) / 2.0, ym)
        .rect(BR_XR - BR_XL, depth)
        .extrude(zp + 10))
plan = plan.edges("|Z").edges(FnSel(lambda e: e.Center().y < BR_Y0 + 0.01)).fillet(R_FRONT_SIDE)

bracket = side.intersect(plan)

# small edge break along the sloped front outline (runs on over the
# shoulders down to the rear face)
top_front = bracket.faces("<Y").edges(
    FnSel(lambda e: _bb(e).zmax > zb + 0.5 and not (_bb(e).xlen < 1e-6 and _bb(e).ylen < 1e-6))).vals()
try:
    bracket = cq.Workplane("XY").add(bracket.val().fillet(R_FRONT_TOP, top_front))
except Exception:
    pass

# ---- window, rear pocket and mounting holes (on the 45 deg axis) ----
ux, uz = math.cos(math.radians(SLOPE)), math.sin(math.radians(SLOPE))
vx, vz = -uz, ux


def rotated_box(cx, cz, L, W, y0, y1):
    return (cq.Workplane("XY").box(L, y1 - y0, W)
            .rotate((0, 0, 0), (0, 1, 0), -SLOPE)
            .translate((cx, (y0 + y1) / 2.0, cz)))


wcx, wcz = WIN_C[0], WIN_C[1] + zt
window = rotated_box(wcx, wcz, WIN_L, WIN_W, BR_Y0 - 5, BR_Y1 + 5)
pocket = rotated_box(wcx, wcz, POCKET_L, POCKET_W, BR_Y1 - POCKET_D, BR_Y1 + 5)
pocket = pocket.edges("|Y").fillet(POCKET_R)
bracket = bracket.cut(window).cut(pocket)

for su in (-1, 1):
    for sv in (-1, 1):
        hx = wcx + su * HOLE_U * ux + sv * HOLE_V * vx
        hz = wcz + su * HOLE_U * uz + sv * HOLE_V * vz
        h = (cq.Workplane("XZ", origin=(0, BR_Y1 + 5, 0))
             .center(hx, hz).circle(HOLE_D / 2).extrude(depth + 10))
        bracket = bracket.cut(h)

# ---- triangular lightening opening below the window ----
# window lower long edge:  z - x*tan = k_w   (z above disc top)
k_w = (WIN_C[1] - WIN_C[0] * tan_s) - (WIN_W / 2.0) / math.cos(math.radians(SLOPE))
k_h = k_w - RIB_T / math.cos(math.radians(SLOPE))     # hypotenuse z = x*tan + k_h
tri = [
    ((TRI_ZB - k_h) / tan_s, TRI_ZB + zt),
    (TRI_XR, TRI_ZB + zt),
    (TRI_XR, TRI_XR * tan_s + k_h + zt),
]
tri_cut = (cq.Workplane("XZ", origin=(0, BR_Y1 + 5, 0))
           .polyline(tri).close().extrude(depth + 10))
tri_cut = tri_cut.edges("|Y").edges(FnSel(lambda e: e.Center().z < TRI_ZB + zt + 1)).fillet(TRI_R)
bracket = bracket.cut(tri_cut)

# =====================================================================
#  Assemble + fillet bracket to disc (left, front and right sides only)
# =====================================================================
result = disc.union(bracket)


def _base_edge(e):
    b = _bb(e)
    if b.zlen > 0.01 or abs(b.zmin - T_DISC) > 0.01:
        return False
    c = e.Center()
    return (BR_XL - 1 < c.x < BR_XR + 1) and (BR_Y0 - 1 < c.y < BR_Y1 - 0.3)


def _base_r(x, y, z):
    return R_BASE_FRONT if abs(y - BR_Y0) < 0.05 else R_BASE_SIDE


try:
    base_edges = [e for e in result.val().Edges() if _base_edge(e)]
    result = cq.Workplane("XY").add(variable_fillet(result.val(), base_edges, _base_r))
except Exception:
    try:
        result = result.edges(FnSel(_base_edge)).fillet(R_BASE_FRONT)
    except Exception:
        pass
